import math
import cadquery as cq

# =====================================================================
#  Stepped dome cap: a spherical base flange carrying six concentric
#  terraces and a small top boss (a "ziggurat" hemisphere), hollowed
#  from below by a hemispherical cavity.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
BASE_R = 60.0            # radius of the base flange at the bottom face
FLANGE_H = 12.0          # height of the base flange
FLANGE_ARC_R = 33.0      # profile radius of the convex (toroidal) flange side
FLANGE_ARC_ZC = 3.0      # height at which the flange side is vertical (arc centre height)

# terrace outer radii (bottom to top, last one is the small top boss)
STEP_RADII = [52.25, 44.6, 36.95, 29.3, 21.65, 13.8, 5.8]
# heights of the flat top of every terrace above the bottom face
STEP_TOPS = [32.55, 42.9, 49.85, 54.8, 58.15, 60.4, 61.5]
# round on the outer top edge of each terrace
STEP_FILLETS = [1.3, 1.1, 1.1, 1.0, 1.0, 0.9, 0.25]

CAV_R = 52.0             # radius of the hemispherical cavity (opening radius)
CAV_Z = 2.0              # centre height of the cavity sphere (slightly above the base)


FLANGE_ARC_CR = BASE_R - math.sqrt(FLANGE_ARC_R ** 2 - FLANGE_ARC_ZC ** 2)


def flange_r(z):
    """radius of the convex flange side at height z (arc through (BASE_R, 0))"""
    return FLANGE_ARC_CR + math.sqrt(FLANGE_ARC_R ** 2 - (z - FLANGE_ARC_ZC) ** 2)


# ---------------- outer profile (r, z) revolved about the Z axis ----------------
z_mid = 0.5 * FLANGE_H
prof = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(BASE_R, 0)
    .threePointArc((flange_r(z_mid), z_mid), (flange_r(FLANGE_H), FLANGE_H))
)

c45 = math.cos(math.radians(45.0))
z_prev = FLANGE_H
for r, zt, f in zip(STEP_RADII, STEP_TOPS, STEP_FILLETS):
    prof = prof.lineTo(r, z_prev).lineTo(r, zt - f)
    # quarter-round on the outer top edge of the terrace
    prof = prof.threePointArc((r - f + f * c45, zt - f + f * c45), (r - f, zt))
    z_prev = zt
prof = prof.lineTo(0, z_prev).close()

outer = prof.revolve(360, (0, 0, 0), (0, 1, 0))

# ---------------- hemispherical cavity opening through the bottom face ----------------
cavity = cq.Workplane("XY").add(
    cq.Solid.makeSphere(CAV_R, pnt=cq.Vector(0, 0, CAV_Z), angleDegrees1=-90, angleDegrees2=90)
)

result = outer.cut(cavity)

VIEW = {"azimuth": 45, "elevation": 26}
